import math
import cadquery as cq

# ------------------------------------------------------------------
# Smooth solid of constant width: a rounded Reuleaux-type profile
# (4 tangent circular arcs per half) revolved about its symmetry axis.
# The revolution axis lies horizontally along (1,-1,0): the rounded
# "apex" points towards +X/-Y, the broad spherical "cap" towards -X/+Y.
# ------------------------------------------------------------------

# ---- driving dimensions (mm) ----
WIDTH = 40.0               # constant width (= bounding cube edge)
APEX_R = 15.0              # rounding radius of the apex (on the axis)
RIM_R = 8.0                # rounding radius of the circular rim
AXIS_AZIMUTH = -45.0       # direction of the apex in the XY plane (deg from +X)

# ---- derived profile geometry (s = along axis, q = radial) ----
L1 = WIDTH - APEX_R - RIM_R          # apex centre -> rim centre distance
L2 = WIDTH - 2.0 * RIM_R             # distance between the two rim centres
HALF_G = math.asin((L2 / 2.0) / L1)  # half opening angle at the apex centre

P1 = (0.0, 0.0)                                   # apex / cap arc centre
P2 = (-L1 * math.cos(HALF_G), L2 / 2.0)           # upper rim centre
P3 = (-L1 * math.cos(HALF_G), -L2 / 2.0)          # lower rim centre


def on_arc(c, r, ang):
    return (c[0] + r * math.cos(ang), c[1] + r * math.sin(ang))


g = HALF_G
apex_pt = on_arc(P1, APEX_R, 0.0)
apex_mid = on_arc(P1, APEX_R, g / 2.0)
apex_end = on_arc(P1, APEX_R, g)

side_mid = on_arc(P3, WIDTH - RIM_R, (g + math.pi / 2.0) / 2.0)
side_end = on_arc(P3, WIDTH - RIM_R, math.pi / 2.0)

rim_mid = on_arc(P2, RIM_R, (math.pi / 2.0 + math.pi - g) / 2.0)
rim_end = on_arc(P2, RIM_R, math.pi - g)

cap_mid = on_arc(P1, WIDTH - APEX_R, math.pi - g / 2.0)
cap_pt = on_arc(P1, WIDTH - APEX_R, math.pi)

half_profile = (
    cq.Workplane("XY")
    .moveTo(*apex_pt)
    .threePointArc(apex_mid, apex_end)   # apex rounding
    .threePointArc(side_mid, side_end)   # flank arc (centred on opposite rim centre)
    .threePointArc(rim_mid, rim_end)     # rim rounding
    .threePointArc(cap_mid, cap_pt)      # broad cap arc (centred on apex centre)
    .close()                             # back along the axis
)

body = half_profile.revolve(360.0, (0, 0, 0), (1, 0, 0))
body = body.rotate((0, 0, 0), (0, 0, 1), AXIS_AZIMUTH)

# centre the bounding cube on the origin
bb = body.val().BoundingBox()
body = body.translate((-bb.center.x, -bb.center.y, -bb.center.z))

result = body
